import cadquery as cq

# =====================================================================
#  Square perforated container / pen holder
#  Open-top thin-walled square box; each of the four side walls carries
#  8 staggered rows of 15 left-pointing triangular perforations whose
#  size swells and shrinks along the row.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 70.2            # outer width = depth of the square box
H = 120.0           # overall height
T = 1.5             # wall and bottom thickness (shelled box)

# perforation layout (identical on all four walls, seen from outside)
N_ROWS = 8          # rows of triangular holes per wall
ROW_PITCH = 14.0    # vertical spacing of rows
ROW_MID = H / 2.0 + 0.4   # height of the middle of the row block
N_PER_ROW = 15      # triangles per row
GAP = 2.15          # clear gap between neighbouring triangles in a row
START_A = 1.67      # start of rows 1,3,5,7 (counted from top), from the wall's left edge
START_B = 3.60      # start of rows 2,4,6,8 (staggered rows)

# triangle size profile: largest in the middle and at the ends of a row,
# smallest a quarter of the way along (linear "triangle wave")
TRI_H_MAX = 7.3     # length of the vertical base of the largest triangle
TRI_H_MIN = 3.5     # length of the vertical base of the smallest triangle
TRI_ASPECT = 0.43   # apex depth / base length  (apex points to the left)
PROFILE_PERIOD = 8  # index distance between two largest triangles

CUT_DEPTH = 1.5 * T  # half-depth of the cutting prisms about the wall mid-plane

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------- box: solid block shelled open at the top ----------------
box = (
    cq.Workplane("XY")
    .rect(W, W)
    .extrude(H)
    .faces(">Z")
    .shell(-T)
)


# ---------------- triangle perforations ----------------
def tri_height(i):
    """Base length of the i-th triangle of a row (triangle-wave profile)."""
    mid = (N_PER_ROW - 1) / 2.0
    d = abs(i - mid) % PROFILE_PERIOD
    half = PROFILE_PERIOD / 2.0
    f = abs(d - half) / half          # 1 at the peaks, 0 at the troughs
    return TRI_H_MIN + (TRI_H_MAX - TRI_H_MIN) * f


def wall_triangles():
    """Triangle outlines in wall coordinates (u from the wall's left edge, z up)."""
    tris = []
    for k in range(N_ROWS):                     # k = 0 is the top row
        z = ROW_MID + ((N_ROWS - 1) / 2.0 - k) * ROW_PITCH
        u = START_A if k % 2 == 0 else START_B  # staggered rows
        for i in range(N_PER_ROW):
            h = tri_height(i)
            w = TRI_ASPECT * h
            # apex on the left, vertical base on the right
            tris.append([(u, z), (u + w, z - h / 2.0), (u + w, z + h / 2.0)])
            u += w + GAP
    return tris


# cutting prisms for the front (-Y) wall; seen from outside, +X is to the right
sk = cq.Workplane("XZ", origin=(0, -W / 2.0 + T / 2.0, 0))
for pts in wall_triangles():
    sk = sk.polyline([(-W / 2.0 + u, z) for (u, z) in pts]).close()
front_cutter = sk.extrude(CUT_DEPTH, both=True).val()

# polar pattern of the wall perforations around the vertical axis
cutters = [
    front_cutter.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), a)
    for a in (0, 90, 180, 270)
]

result = box.cut(cq.Workplane("XY").add(cq.Compound.makeCompound(cutters)))
